import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
AXIS_Z = 41.2          # height of the optical axes (X and Y axes cross at the centre)
BORE_R = 8.3           # through bore radius in front plate / back plate

# card holder (front, -Y)
CH_X = 20.8
CH_Y0, CH_Y1 = -52.1, -23.0
CH_H = 41.2
CH_CH_X = 13.0         # half width of the card channel
CH_FLOOR = 10.7
N_SLOTS = 8
SLOT_PITCH = 3.15
SLOT_T = 1.0
SLOT_X = 17.5

# front plate
FP_Y0, FP_Y1 = -23.0, -20.8
FP_TOP = 61.9
FP_FLAT = 7.45
FP_SHOULDER = 49.0

# saddle (cross cradle)
SD = 15.45
SD_R = 9.3
POST_HOLE_R = 1.5
POST_HOLE_OFF = 12.4

# back plate / side wall
BP_Y0, BP_Y1 = 26.0, 31.2
BB_TOP = 58.6
SW_X0 = 13.3
LOW_TOP = 22.0
SLIT_Y0, SLIT_Y1 = 17.0, 28.0
SLIT_Z0, SLIT_Z1 = 54.4, 56.9

# rail (rear)
RL_X0, RL_X1 = -23.9, 24.3
RL_Y0, RL_Y1 = 31.2, 52.5
RL_H = 10.5
RL_WALL = 8.6

# frame block (+X)
FB_X0, FB_X1 = 15.45, 42.8
FB_Y0, FB_Y1 = -12.7, 26.5
FB_H = 15.0
FB_CH = 8.4

# motor plate (-X)
MP_X0, MP_X1 = -57.3, -51.9
MP_Y = 14.2
MP_TOP = 61.9
MP_SHOULDER = 48.5
MP_REC_R = 13.0

# left tray
LT_X0 = -61.5
LOW_WALL_H = 10.4
BAR_Z0, BAR_Z1 = 23.8, 26.8

# cage (front-left)
CG_X0, CG_X1 = -61.5, -39.7
CG_Y0, CG_Y1 = -66.6, -48.7
CG_H = 32.6
ROD_X, ROD_Y, ROD_R = -34.8, -57.5, 1.6


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def ycyl(x, z, r, y0, y1):
    return (cq.Workplane("XZ", origin=(0, y0, 0)).center(x, z).circle(r)
            .extrude(-(y1 - y0)))


def xcyl(y, z, r, x0, x1):
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(y, z).circle(r)
            .extrude(x1 - x0))


def zcyl(x, y, r, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, z0)).center(x, y).circle(r)
            .extrude(z1 - z0))


# ---------------- card holder ----------------
card = box(-CH_X, CH_X, CH_Y0, CH_Y1 + 0.5, 0, CH_H)
card = card.cut(box(-CH_CH_X, CH_CH_X, CH_Y0 - 1, CH_Y1, CH_FLOOR, CH_H + 1))
FL_H, FL_W = 7.4, 2.2
fl_r = (FL_W ** 2 + FL_H ** 2) / (2 * FL_W)
fl_a = math.atan2(FL_H, fl_r - FL_W) / 2
fl_mx = CH_CH_X + fl_r * (1 - math.cos(fl_a))
fl_mz = CH_H - FL_H + fl_r * math.sin(fl_a)
flare = (cq.Workplane("XZ")
         .moveTo(-CH_CH_X, CH_H - FL_H)
         .threePointArc((-fl_mx, fl_mz), (-CH_CH_X - FL_W, CH_H))
         .lineTo(-CH_CH_X - FL_W, CH_H + 1).lineTo(CH_CH_X + FL_W, CH_H + 1)
         .lineTo(CH_CH_X + FL_W, CH_H)
         .threePointArc((fl_mx, fl_mz), (CH_CH_X, CH_H - FL_H)).close()
         .extrude(-(CH_Y1 - CH_Y0) - 0.5).translate((0, CH_Y0 - 0.5, 0)))
card = card.cut(flare)
for i in range(N_SLOTS):
    yc = CH_Y1 - 3.1 - i * SLOT_PITCH
    card = card.cut(box(-SLOT_X, SLOT_X, yc - SLOT_T / 2, yc + SLOT_T / 2, CH_FLOOR - 1.5, CH_H + 1))

# ---------------- front plate ----------------
fp = (cq.Workplane("XZ")
      .polyline([(-CH_X, 0), (CH_X, 0), (CH_X, FP_SHOULDER), (FP_FLAT, FP_TOP),
                 (-FP_FLAT, FP_TOP), (-CH_X, FP_SHOULDER)]).close()
      .extrude(-(FP_Y1 - FP_Y0)).translate((0, FP_Y0, 0)))
web = box(-CH_X, CH_X, FP_Y1 - 0.1, -SD + 0.1, 0, CH_FLOOR)

# ---------------- saddle ----------------
sad = box(-SD, SD, -SD, SD, 0, AXIS_Z)
sad = sad.cut(ycyl(0, AXIS_Z, SD_R, -30, 30)).cut(xcyl(0, AXIS_Z, SD_R, -30, 30))
for (off, sh) in ((-1.0, -0.8), (1.0, 0.8)):
    mslot = (cq.Workplane("XY", origin=(0, 0, AXIS_Z - SD_R - 7))
             .transformed(rotate=(0, 0, 45)).center(sh, off).slot2D(25.0, 1.6).extrude(20))
    sad = sad.cut(mslot)

# ---------------- back plate, side wall, lower block ----------------
bp = box(-SD, SD, BP_Y0, BP_Y1, 0, BB_TOP)
bp = bp.edges("|Y and <X and >Z").chamfer(1.5)
sw = box(SW_X0, SD, SD - 0.1, BP_Y1, 0, BB_TOP)
sw = sw.edges("|X and >Z and <Y").chamfer(0.8)
low = box(-SD, SD, SD - 0.1, BP_Y1, 0, LOW_TOP)
cove = (cq.Workplane("YZ", origin=(-SD, 0, 0))
        .polyline([(BP_Y0 + 0.1, LOW_TOP - 0.1), (BP_Y0 - 3.0, LOW_TOP - 0.1), (BP_Y0 + 0.1, LOW_TOP + 3.1)])
        .close().extrude(SW_X0 + SD + 0.1))
cove2 = (cq.Workplane("XZ", origin=(0, BP_Y0 + 0.1, 0))
         .polyline([(SW_X0 + 0.1, LOW_TOP - 0.1), (SW_X0 - 3.0, LOW_TOP - 0.1), (SW_X0 + 0.1, LOW_TOP + 3.1)])
         .close().extrude(BP_Y0 - SD + 0.2))
back = bp.union(sw).union(low).union(cove).union(cove2)
back = back.cut(box(-SD - 1, SD + 1, SLIT_Y0, SLIT_Y1, SLIT_Z0, SLIT_Z1))

# ---------------- rail ----------------
rc = 0.5 * (RL_X0 + RL_X1)
RL_FLOOR = 5.5
RL_LIP_H = 7.6
RL_LIP_W = 2.9
RL_SLIT_OFF, RL_SLIT_W = 20.6, 1.4
rail = box(RL_X0, RL_X1, RL_Y0 - 0.1, RL_Y1, 0, RL_H)
rail = rail.cut(box(RL_X0 + RL_WALL, RL_X1 - RL_WALL, RL_Y0 + 0.5, RL_Y1 + 1, RL_FLOOR, RL_H + 1))
rail = rail.cut(box(rc - 4.2, rc + 4.2, RL_Y0 + 0.5, RL_Y1 + 1, 2.5, RL_FLOOR + 0.5))
# lower lips at the inner side of the walls
for sgn in (-1, 1):
    xw = rc + sgn * (0.5 * (RL_X1 - RL_X0) - RL_WALL)
    xl = xw + sgn * RL_LIP_W
    rail = rail.cut(box(min(xw, xl), max(xw, xl), RL_Y0 + 0.5, RL_Y1 + 1, RL_LIP_H, RL_H + 1))
# side walls of the rail continue forward beside the back plate
rail = rail.union(box(RL_X0, RL_X0 + RL_WALL, 14.4, RL_Y0 + 0.1, 0, RL_H))
rail = rail.union(box(SD - 0.1, RL_X1, FB_Y1 - 0.1, RL_Y0 + 0.1, 0, RL_H))
for sgn in (-1, 1):
    xs = rc + sgn * RL_SLIT_OFF
    ys0 = 15.3 if sgn < 0 else 27.5
    # vertical slit in the wall top
    slit = (cq.Workplane("XY", origin=(0, 0, 3.0)).center(xs, 0.5 * (ys0 + RL_Y1 + 3))
            .slot2D(RL_Y1 + 3 - ys0, RL_SLIT_W, angle=90).extrude(RL_H))
    rail = rail.cut(slit)
    # horizontal undercut towards the channel
    xi = rc + sgn * 12.5
    rail = rail.cut(box(min(xs, xi), max(xs, xi), RL_Y0 + 0.5, RL_Y1 + 1, 3.0, 4.6))

# ---------------- frame block ----------------
fb = (cq.Workplane("XY")
      .polyline([(FB_X0 - 0.1, FB_Y0), (FB_X1 - FB_CH, FB_Y0), (FB_X1, FB_Y0 + FB_CH),
                 (FB_X1, FB_Y1 - FB_CH), (FB_X1 - FB_CH, FB_Y1), (FB_X0 - 0.1, FB_Y1)]).close()
      .extrude(FB_H))
fb = fb.cut(box(24.0, 32.5, -9.8, 23.4, -1, FB_H + 1))
fb = fb.cut(zcyl(37.5, 0.2, 2.4, -1, FB_H + 1))
fb = fb.cut(zcyl(37.5, 0.2, 3.6, -1, 2.0))
# low step between the web and the frame block
fb = fb.union(box(FB_X0 - 0.1, CH_X, -SD - 0.2, FB_Y0 + 0.1, 0, CH_FLOOR))
for (y0, y1) in ((-12.7, -2.4), (15.9, 26.5)):
    tab = box(17.6, 20.7, y0, y1, 0, 23.5)
    tab = tab.edges("|Y and >Z").fillet(1.2)
    fb = fb.union(tab)
hook = box(FB_X1 - 0.5, FB_X1 + 2.2, 1.5, 12.1, 8.4, 20.8)
hook = hook.edges("|Y and >Z and >X").fillet(1.0)
hook = hook.edges("|Y and <Z and >X").chamfer(1.8)
fb = fb.union(hook)

# ---------------- motor plate ----------------
mp = (cq.Workplane("YZ")
      .polyline([(-MP_Y, 0), (MP_Y, 0), (MP_Y, MP_SHOULDER), (1.0, MP_TOP),
                 (-1.0, MP_TOP), (-MP_Y, MP_SHOULDER)]).close()
      .extrude(MP_X1 - MP_X0).translate((MP_X0, 0, 0)))
mp = mp.cut(xcyl(0, AXIS_Z, MP_REC_R, MP_X1 - 1.4, MP_X1 + 1))
mp = mp.cut(xcyl(0, AXIS_Z, 6.3, MP_X1 - 1.9, MP_X1 + 1))
# wire channel running down from the recess to the middle bar
mp = mp.cut(box(MP_X1 - 1.4, MP_X1 + 1, -3.6, 3.7, BAR_Z1, AXIS_Z))
for ang in (0, 120, 240):
    a = math.radians(ang)
    hy, hz = 9.8 * math.cos(a), AXIS_Z + 9.8 * math.sin(a)
    mp = mp.cut(xcyl(hy, hz, 1.5, MP_X0 - 1, MP_X1 + 1))
    # counterbore on the outer (-X) face
    mp = mp.cut(xcyl(hy, hz, 2.6, MP_X0 - 1, MP_X0 + 1.0))
for (py, pz) in ((0, AXIS_Z), (-9.5, AXIS_Z)):
    mp = mp.union(xcyl(py, pz, 1.5, MP_X1 - 2.0, MP_X1 + 2.0))

# ---------------- left tray ----------------
side_bar = box(LT_X0, MP_X0 + 0.1, CG_Y1 - 0.1, 14.4, 0, LOW_WALL_H)
back_wall = box(LT_X0, RL_X0 + 0.1, 12.4, 14.4, 0, 7.5)
bars = None
for (y0, y1) in ((9.5, 14.4), (-3.6, 3.7), (-14.4, -9.4)):
    b = box(MP_X1 - 0.1, -SD + 0.1, y0, y1, BAR_Z0, BAR_Z1)
    bars = b if bars is None else bars.union(b)
# low front wall from cage to card holder
FW_Y0, FW_Y1 = -51.2, -49.5
FP_POST_X = -37.0
FW_R = 2.0
front_wall = (cq.Workplane("XZ", origin=(0, FW_Y0, 0))
              .moveTo(CG_X1 - 0.1, 0).lineTo(-CH_X + 0.1, 0).lineTo(-CH_X + 0.1, LOW_WALL_H)
              .lineTo(FP_POST_X + FW_R, LOW_WALL_H)
              .threePointArc((FP_POST_X + FW_R * (1 - math.cos(math.pi / 4)),
                              LOW_WALL_H + FW_R * (1 - math.sin(math.pi / 4))),
                             (FP_POST_X, LOW_WALL_H + FW_R))
              .lineTo(FP_POST_X, CG_H).lineTo(CG_X1 - 0.1, CG_H).close()
              .extrude(-(FW_Y1 - FW_Y0)))
tray_front = box(MP_X1 - 0.1, -SD + 0.1, -14.4, -12.4, 0, LOW_WALL_H)
tray_inner = box(-20.7, -SD + 0.1, -14.4, 14.4, 0, LOW_WALL_H)

# ---------------- cage ----------------
cage = box(CG_X0, CG_X1, CG_Y0, CG_Y1, 0, CG_H)
cage = cage.cut(box(CG_X0 + 2.2, CG_X1 - 2.2, CG_Y0 + 2.2, CG_Y1 - 2.2, 2.5, CG_H - 1.5))
cage = cage.cut(box(CG_X0 + 4.1, CG_X1 - 3.8, CG_Y0 - 1, CG_Y1 + 1, 3.0, CG_H - 1.5)
                .edges("|Y").fillet(2.0))
cage = cage.cut(box(CG_X0 - 1, CG_X1 + 1, CG_Y0 + 2.6, CG_Y1 - 2.6, 3.0, CG_H - 1.5)
                .edges("|X").fillet(2.0))
cage = cage.cut(box(CG_X0 + 3.5, CG_X1 - 3.5, CG_Y0 + 3.5, CG_Y1 - 3.5, -1, 1.0))
# keyhole notch in the top from the +X side
notch = (cq.Workplane("XY", origin=(0, 0, CG_H - 3)).center(CG_X1 - 2.0, ROD_Y)
         .slot2D(6.0, 3.0).extrude(4))
cage = cage.cut(notch)
for (px, py) in ((-57.35, -50.3), (-43.9, -50.3), (-57.35, -64.6), (-43.9, -64.6)):
    cage = cage.union(zcyl(px, py, 0.9, CG_H - 0.1, CG_H + 1.8))
rod = (cq.Workplane("XY").center(ROD_X, ROD_Y).slot2D(4.2, 2 * ROD_R, angle=90).extrude(CG_H))
rod = rod.faces(">Z").edges().fillet(0.7)
rod_foot = box(CG_X1 - 0.1, ROD_X, ROD_Y - 2.1, ROD_Y + 2.1, 0, 3.0)

result = (card.union(fp).union(web).union(sad).union(back).union(rail).union(fb)
          .union(mp).union(side_bar).union(back_wall).union(bars).union(front_wall)
          .union(tray_front).union(tray_inner).union(cage).union(rod).union(rod_foot))
# bore through the front plate, saddle and back plate
result = result.cut(ycyl(0, AXIS_Z, BORE_R, -30, 40))
# rear screw holes in the back plate
for (hx, hz) in ((8.9, 10.2), (8.9, -14.6), (-8.9, -14.6)):
    result = result.cut(ycyl(hx, AXIS_Z + hz, 1.3, BP_Y1 - 3.5, BP_Y1 + 1))
# saddle post holes
for sx in (-1, 1):
    for sy in (-1, 1):
        result = result.cut(zcyl(sx * POST_HOLE_OFF, sy * POST_HOLE_OFF, POST_HOLE_R, -1, AXIS_Z + 1))
        result = result.cut(zcyl(sx * POST_HOLE_OFF, sy * POST_HOLE_OFF, 2.1, AXIS_Z - 0.8, AXIS_Z + 1))
